import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 120.0          # overall width (X)
D = 35.5           # overall depth (Y), front face at -D/2
H = 65.0           # height at the front (top at z=H, front-bottom edge at z=0)
SLOPE = 10.0       # bottom face rises toward the back (deg)

R_CORNER = 12.0    # rounding of the 4 edges running front-to-back
R_FRONT = 7.0      # fillet around the front face perimeter

# display window (through the front wall)
WIN_W = 74.7
WIN_H = 38.8
WIN_ZC = 35.5      # window centre height
WIN_CH = 2.4       # chamfer on the front edge of the window

# cavity open to the back
T_FRONT = 2.6      # front wall thickness
T_TOP = 5.5        # top wall
CAV_Z0 = 13.0      # cavity floor height
T_PX = 9.7         # +X end wall
T_NX = 18.0        # -X end wall (thick, carries two screws)

# notch in the thick -X wall
NOTCH_T = 6.1      # remaining wall in notch
NOTCH_Z0 = 26.8
NOTCH_Z1 = 45.3

# screw holes in the back face
HOLE_D = 5.0
HOLE_DEPTH = 8.0
HOLE_X_NX = -W / 2 + 8.7          # two holes in the thick -X wall
HOLES = [(HOLE_X_NX, 58.5), (HOLE_X_NX, 13.7), (W / 2 - T_PX / 2, 36.0)]

# ---------------- outer body ----------------
zb = D * math.tan(math.radians(SLOPE))   # bottom height at the back
profile = [(-D / 2, 0.0), (D / 2, zb), (D / 2, H), (-D / 2, H)]
body = (
    cq.Workplane("YZ", origin=(-W / 2, 0, 0))
    .polyline(profile).close()
    .extrude(W)
)

# round the four long edges (front-to-back) between the end faces and top/bottom
def end_edges(wp):
    return wp.edges(
        cq.selectors.SumSelector(
            cq.selectors.SumSelector(
                cq.selectors.NearestToPointSelector((W / 2, 0, H)),
                cq.selectors.NearestToPointSelector((-W / 2, 0, H)),
            ),
            cq.selectors.SumSelector(
                cq.selectors.NearestToPointSelector((W / 2, 0, zb / 2)),
                cq.selectors.NearestToPointSelector((-W / 2, 0, zb / 2)),
            ),
        )
    )


body = end_edges(body).fillet(R_CORNER)
body = body.faces("<Y").edges().fillet(R_FRONT)

# ---------------- window ----------------
win = (
    cq.Workplane("XZ", origin=(0, 0, WIN_ZC))
    .rect(WIN_W, WIN_H)
    .extrude(-(T_FRONT + 2))  # XZ normal is -Y, negative extrude goes +Y
    .translate((0, -D / 2 - 1, 0))
)
body = body.cut(win)
body = body.faces("<Y").edges(cq.selectors.BoxSelector(
    (-WIN_W / 2 - 1, -D / 2 - 1, WIN_ZC - WIN_H / 2 - 1),
    (WIN_W / 2 + 1, -D / 2 + 1, WIN_ZC + WIN_H / 2 + 1))).chamfer(WIN_CH)

# ---------------- cavity from the back ----------------
cx0 = -W / 2 + T_NX
cx1 = W / 2 - T_PX
cz1 = H - T_TOP
cav = cq.Workplane("XY").box(cx1 - cx0, D, cz1 - CAV_Z0, centered=False).translate(
    (cx0, -D / 2 + T_FRONT, CAV_Z0))
body = body.cut(cav)

notch = cq.Workplane("XY").box(T_NX - NOTCH_T + 0.01, D, NOTCH_Z1 - NOTCH_Z0, centered=False).translate(
    (-W / 2 + NOTCH_T, -D / 2 + T_FRONT, NOTCH_Z0))
body = body.cut(notch)

# ---------------- screw holes in the back face ----------------
for (hx, hz) in HOLES:
    h = cq.Workplane("XZ", origin=(hx, D / 2 + 1, hz)).circle(HOLE_D / 2).extrude(HOLE_DEPTH + 1)
    body = body.cut(h)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
